import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
BOX_W = 31.0      # box width  (X)
BOX_D = 16.0      # box depth  (Y)
BOX_H = 100.0     # box height (Z)
WALL = 2.0        # shell wall thickness (box is open on the -X side)

WIN_X = 23.0      # window in +Y wall spans X in [0, WIN_X]
WIN_Z0 = 8.5      # window bottom
WIN_Z1 = 40.5     # window top

ROD_D = 6.4                 # plain rod diameter
ROD_X = 27.5                # rod axis X position
ROD_Z = 50.4                # rod axis height
ROD_LEN = 103.4             # from +Y face of box to elbow point
THREAD_LEN = 15.6           # threaded length next to the box
THREAD_OD = 6.3             # thread crest diameter
THREAD_CORE_D = 4.5         # thread root diameter
THREAD_RIDGES = 8

ARM_D = 6.4                 # diagonal arm diameter
ARM_CAP = 2.6               # arm overhang beyond elbow point
ROD_OVER = 0.6              # rod overhang beyond elbow point (+Y)

CUP_D = 17.4                # cup outer diameter
CUP_L = 12.6                # cup length along Y
CUP_X = 1.5                 # cup axis X
CUP_Z = 24.5                # cup axis Z
CUP_BORE_D = 14.4           # cup bore (open towards -Y)
CUP_BORE_DEPTH = 11.0

VIEW = {"azimuth": 45, "elevation": 26}

Y_AXIS = cq.Vector(0, 1, 0)


def wp(shape):
    return cq.Workplane("XY").add(shape)


def cylinder(radius, length, origin, axis, seam_dir):
    """Plain cylinder; seam_dir picks where the B-rep seam line lies."""
    pl = cq.Plane(origin=tuple(origin), xDir=tuple(seam_dir), normal=tuple(axis))
    return cq.Workplane(pl).circle(radius).extrude(length).val()


# seam direction for cylinders along Y: down and towards -X (hidden in most views)
SEAM_Y = cq.Vector(-0.55, 0.0, -0.835).normalized()


def y_cylinder(radius, y_start, length, x, z):
    return cylinder(radius, length, cq.Vector(x, y_start, z), Y_AXIS, SEAM_Y)


# ---------------- box (thin shell, open at -X) ----------------
box = (
    cq.Workplane("XY")
    .box(BOX_W, BOX_D, BOX_H, centered=False)
    .faces("<X")
    .shell(-WALL)
)
window = cq.Workplane("XY").box(
    WIN_X + 1.0, WALL + 2.0, WIN_Z1 - WIN_Z0, centered=False
).translate((-1.0, BOX_D - WALL - 1.0, WIN_Z0))
box = box.cut(window)

# ---------------- rod with threaded section ----------------
y0 = BOX_D
y_el = BOX_D + ROD_LEN

rod = wp(y_cylinder(ROD_D / 2.0, y0 + THREAD_LEN, y_el + ROD_OVER - (y0 + THREAD_LEN), ROD_X, ROD_Z))

# thread modelled as plain rounded ridges: one revolved profile of circular arcs
pitch = THREAD_LEN / THREAD_RIDGES
r_root = THREAD_CORE_D / 2.0
r_crest = THREAD_OD / 2.0
prof = cq.Workplane("XZ").moveTo(0, -0.3).lineTo(r_root, -0.3).lineTo(r_root, 0)
for i in range(THREAD_RIDGES):
    ya = pitch * i
    prof = prof.threePointArc((r_crest, ya + pitch / 2.0), (r_root, ya + pitch))
thread = (
    prof.lineTo(0, THREAD_LEN)
    .close()
    .revolve(360, (0, 0, 0), (0, 1, 0))
    .rotate((0, 0, 0), (1, 0, 0), -90)
    .rotate((0, 0, 0), (0, 1, 0), math.degrees(math.atan2(-SEAM_Y.z, SEAM_Y.x)))
    .translate((ROD_X, y0, ROD_Z))
)

# ---------------- diagonal arm ----------------
adir = cq.Vector(CUP_X - ROD_X, 0, CUP_Z - ROD_Z)
arm_len_to_center = adir.Length
adir = adir.normalized()
arm_start = cq.Vector(ROD_X, y_el, ROD_Z) - adir * ARM_CAP
arm_len = ARM_CAP + arm_len_to_center - CUP_D / 2.0 + 1.0
arm = wp(cylinder(ARM_D / 2.0, arm_len, arm_start, adir, Y_AXIS))

# ---------------- cup ----------------
cup = wp(y_cylinder(CUP_D / 2.0, y_el - CUP_L / 2.0, CUP_L, CUP_X, CUP_Z))

result = box.union(thread).union(rod).union(arm).union(cup)

bore = y_cylinder(
    CUP_BORE_D / 2.0, y_el - CUP_L / 2.0 - 0.5, CUP_BORE_DEPTH + 0.5, CUP_X, CUP_Z
)
result = result.cut(wp(bore))

